import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0        # outer size along X
D = 101.6        # outer size along Y
H = 48.0         # overall height
T = 3.2          # wall thickness
T_FLOOR = 2.9    # floor thickness
R_OUT = 2.8      # vertical outer corner radius
R_BOT = 1.0      # small round on the bottom outer edges

# slots (U-shaped, open at the top)
SLOT_Z = 13.9                    # height of slot bottom above the base
SLOT_A = (-37.35, -15.2)         # Y range of slot through both X walls
SLOT_B = (12.25, 32.06)          # Y range of 2nd slot (+X wall only)
STEP_H = 5.8                     # depth of the relief at the top of the middle web
STEP_W = 0.45                    # lateral relief per side

# corner bosses
BOSS = 8.3                       # boss size (X and Y)
BOSS_DY_TAB = 8.6                # depth (Y) of the boss in front of a tab
BOSS_TOP = 11.35                 # boss top height (absolute Z)
BOSS_R = 3.5                     # rounded inner corner of boss
TAB_T = 5.0                      # thickness of the tall tab at the +Y corners
TAB_TOP = 20.9                   # tab top height (absolute Z)
TAB_R = 1.8                      # round on the tab top front edge
PIN_D = 3.6
PIN_H = 2.8
PIN_R = 1.0
PIN_OFF = 4.65                   # pin centre offset from walls
EMBED = 0.5                      # bosses are sunk into walls/floor for a clean union

# polarity marks and small hole
MARK_Z = 8.7
MARK_DY = 5.5                    # +/- offset from slot centre
MARK_L = 5.4
MARK_W = 1.1
MARK_DEPTH = 0.5
HOLE_D = 2.2
HOLE_Y = -17.5
HOLE_Z = 11.3

# ---------------- derived ----------------
XI = W / 2 - T      # inner half sizes
YI = D / 2 - T

# ---------------- outer shell ----------------
body = (
    cq.Workplane("XY")
    .rect(W, D)
    .extrude(H)
    .edges("|Z").fillet(R_OUT)
    .faces("<Z").edges().fillet(R_BOT)
)

pocket = (
    cq.Workplane("XY", origin=(0, 0, T_FLOOR))
    .rect(2 * XI, 2 * YI)
    .extrude(H)
)
body = body.cut(pocket)

# ---------------- slots ----------------
def box(x0, x1, y0, y1, z0, z1):
    return (
        cq.Workplane("XY", origin=((x0 + x1) / 2, (y0 + y1) / 2, z0))
        .rect(abs(x1 - x0), abs(y1 - y0))
        .extrude(z1 - z0)
    )

slot_cut = box(-W, W, SLOT_A[0], SLOT_A[1], SLOT_Z, H + 1)          # both X walls
slot_cut = slot_cut.union(box(0, W, SLOT_B[0], SLOT_B[1], SLOT_Z, H + 1))
# relief at the top of the middle web of the +X wall
slot_cut = slot_cut.union(box(0, W, SLOT_A[1] - 1, SLOT_A[1] + STEP_W, H - STEP_H, H + 1))
slot_cut = slot_cut.union(box(0, W, SLOT_B[0] - STEP_W, SLOT_B[0] + 1, H - STEP_H, H + 1))
body = body.cut(slot_cut)

# ---------------- corner bosses ----------------
def lower_boss(sx, sy, depth_y, offset_y):
    """Block in corner (sx, sy) with rounded inner corner.
    offset_y: distance from the Y wall where the block starts."""
    x_wall = sx * XI
    y_wall = sy * YI
    x0, x1 = sorted((x_wall + sx * EMBED, x_wall - sx * BOSS))
    y_start = y_wall - sy * offset_y
    y_back = y_start + sy * EMBED
    y0, y1 = sorted((y_back, y_start - sy * depth_y))
    blk = box(x0, x1, y0, y1, T_FLOOR - EMBED, BOSS_TOP)
    # round the inner vertical corner (the one facing the box centre)
    xc = x_wall - sx * BOSS
    yc = y_start - sy * depth_y
    blk = blk.edges("|Z").edges(
        cq.selectors.NearestToPointSelector((xc, yc, (BOSS_TOP + T_FLOOR) / 2))
    ).fillet(BOSS_R)
    return blk


def pin(px, py):
    p = (
        cq.Workplane("XY", origin=(px, py, BOSS_TOP - 0.01))
        .circle(PIN_D / 2)
        .extrude(PIN_H + 0.01)
        .faces(">Z").edges().fillet(PIN_R)
    )
    return p


features = None
for sx in (-1, 1):
    # -Y corners : plain boss with pin
    sy = -1
    b = lower_boss(sx, sy, BOSS, 0.0)
    b = b.union(pin(sx * (XI - PIN_OFF), sy * (YI - PIN_OFF)))
    features = b if features is None else features.union(b)

    # +Y corners : tall tab against the +Y wall plus boss in front of it
    sy = 1
    x0, x1 = sorted((sx * (XI + EMBED), sx * (XI - BOSS)))
    tab = box(x0, x1, YI - TAB_T, YI + EMBED, T_FLOOR - EMBED, TAB_TOP)
    tab = tab.edges("|X").edges(
        cq.selectors.NearestToPointSelector((sx * (XI - BOSS / 2), YI - TAB_T, TAB_TOP))
    ).fillet(TAB_R)
    b = lower_boss(sx, sy, BOSS_DY_TAB, TAB_T)
    b = b.union(tab)
    b = b.union(pin(sx * (XI - PIN_OFF), YI - TAB_T - PIN_OFF))
    features = features.union(b)

body = body.union(features)

# ---------------- polarity marks on +X face ----------------
yc_a = (SLOT_A[0] + SLOT_A[1]) / 2
plus_y = yc_a - MARK_DY
minus_y = yc_a + MARK_DY
xm0, xm1 = W / 2 - MARK_DEPTH, W / 2 + 1
marks = box(xm0, xm1, plus_y - MARK_L / 2, plus_y + MARK_L / 2,
            MARK_Z - MARK_W / 2, MARK_Z + MARK_W / 2)
marks = marks.union(box(xm0, xm1, plus_y - MARK_W / 2, plus_y + MARK_W / 2,
                        MARK_Z - MARK_L / 2, MARK_Z + MARK_L / 2))
marks = marks.union(box(xm0, xm1, minus_y - MARK_L / 2, minus_y + MARK_L / 2,
                        MARK_Z - MARK_W / 2, MARK_Z + MARK_W / 2))
body = body.cut(marks)

# ---------------- small hole in -X wall ----------------
hole = (
    cq.Workplane("YZ", origin=(-W / 2 - 1, HOLE_Y, HOLE_Z))
    .circle(HOLE_D / 2)
    .extrude(T + 2)
)
body = body.cut(hole)

result = body
assert result.val().isValid()

VIEW = {"azimuth": 45, "elevation": 26}
